import math
import cadquery as cq

# =====================================================================
# Bracket: thick top flange with two tapered-hole ears, a hollow
# stadium-shaped body hanging underneath whose back/bottom is swept
# away (flat vertical front face, inclined + filleted back), open at
# the swept face (shelled), row of holes through the flange.
# X = length, Y = depth (front face at -Y), Z = up.
# =====================================================================

# ---------------- overall ----------------
H = 31.2              # overall height
T = 12.0              # flange thickness
BODY_HALF_LEN = 35.6  # body half length in X (stadium ends)
BODY_R = 11.6         # body half depth = stadium end radius (depth 23.2)

# ---------------- ears ----------------
EAR_X = 41.0          # ear centre X (+/-)
EAR_Y = 7.0           # ear centre Y (ears sit toward the back)
EAR_R = 9.2           # ear outer radius
EAR_BACK_PT = (27.2, BODY_R)   # back tangent line of the ear meets the body here
EAR_FRONT_PT = (34.0, -5.9)    # front tangent line of the ear meets the body here

# ---------------- side profile (seen from +X) ----------------
BAND = 14.4           # depth from top of the horizontal back under-surface
BOT_FLAT = 2.23       # width of the flat bottom strip behind the front face
SLOPE = 0.553         # dY/dZ of the inclined back face
FILLET_R = 9.4        # radius blending incline into the horizontal under-surface

# ---------------- hollow ----------------
WALL = 2.2            # wall thickness of the hollow body (open at the swept face)

# ---------------- holes ----------------
EAR_HOLE_RT = 5.35    # ear hole: top radius of the conical part
EAR_HOLE_RB = 3.35    # ear hole: straight bore radius
EAR_CONE_D = 4.5      # depth of the conical part
BIG_HOLE_R = 7.75     # two blind holes, concentric with the stadium ends
BIG_HOLE_DEPTH = 10.0
SM_CB_R = 4.75        # three small holes: large bore radius
SM_CB_DEPTH = 10.0    # ... its depth
SM_R = 3.9            # ... through radius into the hollow
SM_PTS = [(-10.8, 5.0), (0.0, 0.0), (10.8, -5.0)]

ZT = H                # top face height
ZP = H - T            # flange underside height
SLOT_C = BODY_HALF_LEN - BODY_R   # X of the stadium end centres


# ---------------- body: stadium prism ----------------
body = cq.Workplane("XY").slot2D(2 * BODY_HALF_LEN, 2 * BODY_R).extrude(H)


# ---------------- ears (tabs) ----------------
def _tangent(p, c, r, upper):
    """tangent point on circle (c, r) of a line through p; upper/lower one"""
    dx, dy = p[0] - c[0], p[1] - c[1]
    d = math.hypot(dx, dy)
    phi = math.atan2(dy, dx)
    a = math.acos(r / d)
    cands = []
    for ang in (phi + a, phi - a):
        cands.append((c[0] + r * math.cos(ang), c[1] + r * math.sin(ang)))
    cands.sort(key=lambda q: q[1])
    return cands[1] if upper else cands[0]


def ear_tab(sign):
    c = (EAR_X, EAR_Y)
    tb = _tangent(EAR_BACK_PT, c, EAR_R, True)
    tf = _tangent(EAR_FRONT_PT, c, EAR_R, False)
    ab = math.atan2(tb[1] - c[1], tb[0] - c[0])
    af = math.atan2(tf[1] - c[1], tf[0] - c[0])
    am = 0.5 * (ab + af)            # passes through the outer end of the ear
    m = (c[0] + EAR_R * math.cos(am), c[1] + EAR_R * math.sin(am))

    def s(p):
        return (sign * p[0], p[1])

    return (
        cq.Workplane("XY", origin=(0, 0, ZP))
        .moveTo(*s(EAR_BACK_PT))
        .lineTo(*s(tb))
        .threePointArc(s(m), s(tf))
        .lineTo(*s(EAR_FRONT_PT))
        .lineTo(*s((SLOT_C, 0.0)))
        .lineTo(*s((SLOT_C, BODY_R)))
        .close()
        .extrude(T)
    )


part = body.union(ear_tab(1)).union(ear_tab(-1))

# ---------------- swept-away back of the body ----------------
# profile in the YZ plane (Z up from the bottom face)
yb0 = -BODY_R + BOT_FLAT               # incline starts here on the bottom
zh = H - BAND                          # horizontal under-surface height
yc = yb0 + SLOPE * zh                  # incline / horizontal corner
L = math.hypot(SLOPE, 1.0)
ux, uz = -SLOPE / L, -1.0 / L          # unit vector down the incline
theta = math.acos(ux)                  # angle between incline and +Y
tdist = FILLET_R / math.tan(theta / 2.0)
p_h = (yc + tdist, zh)                 # fillet tangent point on the horizontal
p_i = (yc + ux * tdist, zh + uz * tdist)   # fillet tangent point on the incline
bx, bz = 1.0 + ux, uz                  # bisector direction
bl = math.hypot(bx, bz)
bx, bz = bx / bl, bz / bl
dc = FILLET_R / math.sin(theta / 2.0)
cc = (yc + bx * dc, zh + bz * dc)      # fillet centre
mx, mz = yc - cc[0], zh - cc[1]
ml = math.hypot(mx, mz)
p_m = (cc[0] + FILLET_R * mx / ml, cc[1] + FILLET_R * mz / ml)

SPAN = 200.0
cutter = (
    cq.Workplane("YZ", origin=(-SPAN / 2, 0, 0))
    .moveTo(yb0, -1.0)
    .lineTo(yb0, 0.0)
    .lineTo(*p_i)
    .threePointArc(p_m, p_h)
    .lineTo(BODY_R + 10.0, zh)
    .lineTo(BODY_R + 10.0, -1.0)
    .close()
    .extrude(SPAN)
)
part = part.cut(cutter)

# ---------------- hollow: body shelled, open at the swept face ----------------
cavity = (
    cq.Workplane("XY", origin=(0, 0, -1.0))
    .slot2D(2 * (BODY_HALF_LEN - WALL), 2 * (BODY_R - WALL))
    .extrude(ZP + 1.0)
)
part = part.cut(cavity)

# ---------------- ear holes: conical mouth + straight bore ----------------
for sx in (-1, 1):
    cone = cq.Solid.makeCone(
        EAR_HOLE_RB, EAR_HOLE_RT, EAR_CONE_D + 0.01,
        pnt=cq.Vector(sx * EAR_X, EAR_Y, ZT - EAR_CONE_D), dir=cq.Vector(0, 0, 1),
    )
    bore = cq.Solid.makeCylinder(
        EAR_HOLE_RB, T + 2.0, pnt=cq.Vector(sx * EAR_X, EAR_Y, ZP - 1.0),
        dir=cq.Vector(0, 0, 1),
    )
    part = part.cut(cq.Workplane().add(cone)).cut(cq.Workplane().add(bore))

# ---------------- blind holes over the stadium ends ----------------
part = (
    part.faces(">Z").workplane(origin=(0, 0, ZT))
    .pushPoints([(-SLOT_C, 0.0), (SLOT_C, 0.0)])
    .hole(2 * BIG_HOLE_R, BIG_HOLE_DEPTH)
)

# ---------------- stepped holes into the hollow ----------------
part = (
    part.faces(">Z").workplane(origin=(0, 0, ZT))
    .pushPoints(SM_PTS)
    .cboreHole(2 * SM_R, 2 * SM_CB_R, SM_CB_DEPTH, depth=T + 1.0)
)

result = part

VIEW = {"azimuth": 45, "elevation": 26}
